import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0        # length along X
W = 150.0        # outer width along Y (across the two walls)
H = 35.5         # wall height (Z)
T = 2.5          # sheet thickness
RI = 3.0         # inner bend radius
RO = RI + T      # outer bend radius
YI = W / 2 - T   # |Y| of wall inner faces

# wall vent slots (13 per wall, running down through the bend into the base)
N_SLOT = 13
SLOT_W = 2.9
SLOT_PITCH = 5.73
SLOT_X0 = -43.05            # centre X of the first slot
SLOT_TOP = H - 5.8          # Z of slot top
SLOT_BASE_END = 67.0        # |Y| where the slot ends in the base

# notch in the top edge of each wall
NOTCH_X0, NOTCH_X1, NOTCH_D = 38.0, 48.3, 2.4

# base openings
WIN_X0, WIN_X1, WIN_Y0, WIN_Y1 = -55.4, 3.9, -41.1, 46.0   # large window
END_X0, END_X1, END_Y = 37.7, 57.2, 63.5                   # slot near +X end

# knock-out slot rings in the base
KO_W = 1.3

# dimples
DIMPLE_D = 7.0
DIMPLE_DEPTH = 0.35
DIMPLES = [(-50.0, 65.6), (32.4, 65.6), (-49.9, -57.0), (32.7, -57.0)]


# ---------------- U channel ----------------
def u_profile():
    a = W / 2
    wp = (
        cq.Workplane("YZ")
        .moveTo(-a, H)
        .lineTo(-a, RO)
        .radiusArc((-a + RO, 0), -RO)
        .lineTo(a - RO, 0)
        .radiusArc((a, RO), -RO)
        .lineTo(a, H)
        .lineTo(a - T, H)
        .lineTo(a - T, T + RI)
        .radiusArc((a - T - RI, T), RI)
        .lineTo(-a + T + RI, T)
        .radiusArc((-a + T, T + RI), RI)
        .lineTo(-a + T, H)
        .close()
    )
    return wp.extrude(L).translate((-L / 2, 0, 0))


def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


body = u_profile()

# ---------------- end details: rims, ledges, lips and tabs ----------------
RIM_X = -55.4       # inner X of the raised base rim along the -X end
LIP_Y0, LIP_Y1 = 50.5, 67.0   # |Y| span of the upturned lip at the -X end
LIP_TOP = 7.5       # Z of lip top
LEDGE_TOP = 4.5     # Z of the -X base rim top
NT_X0, NT_X1 = -57.5, -55.3   # X span of the -X end latch tab / top hook
NT_P = 2.6          # their protrusion from the wall inner face
NT_BOT, NT_TOP = 16.7, 31.6   # latch tab Z span
NH_BOT, NH_TOP = 33.4, 34.9   # top hook Z span
NR_X0 = -56.7       # X start of the narrow rim below the -X latch tab
NR_P = 1.0          # its protrusion
XR_X0, XR_X1 = 54.6, 56.3     # X span of the +X end rib
XR_P = 2.0          # rib protrusion from the wall inner face
XR_H = 1.8          # rib height above the base
XR_R = 1.5          # rib inner corner radius
XT_P = 4.4          # latch tab protrusion from the wall inner face
XT_BOT, XT_TOP = 16.8, 31.6   # latch tab Z span
XT_V = 1.2          # length of the pointed tab ends
D_Y1 = 65.3         # |Y| of the straight (wall side) edge of the D-tab
D_R = 2.8           # D-tab radius (= width)
D_TOP = 7.8         # D-tab top Z
adds = []
for s in (-1, 1):
    yi = YI
    # -X end: raised rim on the base from the window edge up to the wall
    ledge_in = WIN_Y1 if s > 0 else -WIN_Y0
    y_a, y_b = sorted((s * ledge_in, s * (yi - 0.01)))
    adds.append(box(-L / 2, RIM_X, y_a, y_b, T - 0.5, LEDGE_TOP))
    # -X end: upturned lip
    y_a, y_b = sorted((s * LIP_Y0, s * LIP_Y1))
    lip = box(RIM_X - 1.9, RIM_X - 0.1, y_a, y_b, T - 0.5, LIP_TOP)
    lip = lip.faces(">Z").edges("|Y").fillet(0.6)
    adds.append(lip)
    # -X end latch tab and top hook on the wall inner face
    y_a, y_b = sorted((s * (yi + 0.5), s * (yi - NT_P)))
    tab = box(NT_X0, NT_X1, y_a, y_b, NT_BOT, NT_TOP)
    tab = tab.faces("<Z").edges("|X").edges("<Y" if s > 0 else ">Y").chamfer(1.5)
    adds.append(tab)
    hook = box(NT_X0, NT_X1, y_a, y_b, NH_BOT, NH_TOP)
    hook = hook.faces(">Z").edges("|X").edges("<Y" if s > 0 else ">Y").fillet(0.6)
    adds.append(hook)
    # -X end narrow rim running from the latch tab down into the bend
    rim = (
        cq.Workplane("YZ")
        .polyline([(yi + 0.5, T - 0.5), (yi + 0.5, NT_BOT + 0.5), (yi - NR_P, NT_BOT + 0.5),
                   (yi - NR_P, LEDGE_TOP + 1.5)])
        .radiusArc((yi - NR_P - 1.5, LEDGE_TOP), 1.5)
        .lineTo(yi - NR_P - 1.5, T - 0.5)
        .close()
        .extrude(NT_X1 - NR_X0)
        .translate((NR_X0, 0, 0))
    )
    if s < 0:
        rim = rim.mirror("XZ")
    adds.append(rim)
    # +X end: L-shaped rib following the inside of the U near each wall, carrying
    # a pointed latch tab high on the wall and a small D-shaped tab beside the end slot
    pts = [
        (yi + 0.5, T - 0.5),
        (yi + 0.5, H),
        (yi - XR_P, H),
        (yi - XR_P, XT_TOP),
        (yi - XT_P, XT_TOP - XT_V),
        (yi - XT_P, XT_BOT + XT_V),
        (yi - XR_P, XT_BOT),
        (yi - XR_P, T + XR_H + XR_R),
    ]
    prof = (
        cq.Workplane("YZ")
        .polyline(pts)
        .radiusArc((yi - XR_P - XR_R, T + XR_H), XR_R)
        .lineTo(D_Y1, T + XR_H)
        .lineTo(D_Y1, D_TOP)
        .threePointArc(
            (D_Y1 - D_R * 0.7071, D_TOP - D_R + D_R * 0.7071), (D_Y1 - D_R, D_TOP - D_R)
        )
        .lineTo(D_Y1 - D_R, T + XR_H)
        .lineTo(END_Y, T + XR_H)
        .lineTo(END_Y, T - 0.5)
        .close()
    )
    rib = prof.extrude(XR_X1 - XR_X0).translate((XR_X0, 0, 0))
    if s < 0:
        rib = rib.mirror("XZ")
    adds.append(rib)

for a in adds:
    body = body.union(a)

# ---------------- wall slots ----------------
cutters = None
for side in (-1, 1):
    for i in range(N_SLOT):
        x = SLOT_X0 + i * SLOT_PITCH
        ylen = W / 2 + 1 - SLOT_BASE_END
        yc = side * (SLOT_BASE_END + ylen / 2)
        c = (
            cq.Workplane("XY")
            .box(SLOT_W, ylen, SLOT_TOP + 1, centered=(True, True, False))
            .translate((x, yc, -1))
        )
        # round the inner end (in plan) and the top end (in elevation)
        c = c.edges("|Z").edges("<Y" if side > 0 else ">Y").fillet(SLOT_W / 2 - 0.05)
        c = c.faces(">Z").edges("|Y").fillet(0.8)
        cutters = c if cutters is None else cutters.union(c)
body = body.cut(cutters)

# ---------------- notches ----------------
for side in (-1, 1):
    y_a, y_b = sorted((side * (YI - 1.0), side * (W / 2 + 1.0)))
    body = body.cut(box(NOTCH_X0, NOTCH_X1, y_a, y_b, H - NOTCH_D, H + 1))

# ---------------- base openings ----------------
body = body.cut(box(WIN_X0, WIN_X1, WIN_Y0, WIN_Y1, -1, 10))
body = body.cut(box(END_X0, END_X1, -END_Y, END_Y, -1, T + 0.01))


# ---------------- knock-out slot rings ----------------
def ring(x0, x1, y0, y1, gaps, r=1.2):
    """slot ring of width KO_W around rectangle, with bridges (gaps) removed"""
    w, h = x1 - x0, y1 - y0
    cx, cy = (x0 + x1) / 2, (y0 + y1) / 2
    outer = (
        cq.Workplane("XY").box(w, h, 10).edges("|Z").fillet(r).translate((cx, cy, 0))
    )
    inner = (
        cq.Workplane("XY")
        .box(w - 2 * KO_W, h - 2 * KO_W, 12)
        .edges("|Z")
        .fillet(max(r - KO_W, 0.2))
        .translate((cx, cy, 0))
    )
    rg = outer.cut(inner)
    for gx0, gx1, gy0, gy1 in gaps:
        rg = rg.cut(box(gx0, gx1, gy0, gy1, -6, 6))
    return rg


G = 1.3  # bridge width
kos = []
# two "C = C" rings near the +Y wall
for x0, x1 in ((-53.7, -30.9), (-22.6, 5.6)):
    y0, y1 = 53.1, 60.3
    gl = x0 + 4.4
    gr = x1 - 4.4
    kos.append(
        ring(
            x0, x1, y0, y1,
            [
                (gl, gl + G, y0 - 1, y0 + 2),
                (gl, gl + G, y1 - 2, y1 + 1),
                (gr - G, gr, y0 - 1, y0 + 2),
                (gr - G, gr, y1 - 2, y1 + 1),
            ],
        )
    )
# long ring near the -Y wall
x0, x1, y0, y1 = -46.9, 29.3, -61.8, -52.1
xm, ym = (x0 + x1) / 2, (y0 + y1) / 2
kos.append(
    ring(
        x0, x1, y0, y1,
        [
            (xm - G / 2, xm + G / 2, y0 - 1, y0 + 2),
            (xm - G / 2, xm + G / 2, y1 - 2, y1 + 1),
            (x0 - 1, x0 + 2, ym - G / 2, ym + G / 2),
            (x1 - 2, x1 + 1, ym - G / 2, ym + G / 2),
        ],
    )
)
# small square ring
x0, x1, y0, y1 = 15.5, 27.7, -48.0, -31.4
kos.append(
    ring(
        x0, x1, y0, y1,
        [
            (x0 + 6.0, x0 + 6.0 + G, y1 - 2, y1 + 1),
            (x0 + 4.9, x0 + 4.9 + G, y0 - 1, y0 + 2),
            (x0 - 1, x0 + 2, y0 + 8.2, y0 + 8.2 + G),
            (x1 - 2, x1 + 1, y0 + 7.0, y0 + 7.0 + G),
        ],
        r=0.8,
    )
)
for k in kos:
    body = body.cut(k)

# ---------------- dimples ----------------
for x, y in DIMPLES:
    body = body.cut(
        cq.Workplane("XY")
        .circle(DIMPLE_D / 2)
        .extrude(DIMPLE_DEPTH + 1)
        .translate((x, y, T - DIMPLE_DEPTH))
    )

result = body
